import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
BLOCK_X = 54.0          # width  (X)
BLOCK_Y = 100.0         # length (Y)
BLOCK_H = 11.0          # thickness (Z); underside at z = 0, top at z = BLOCK_H

# post with three gussets (hangs below the underside)
POST_Y = -24.0
POST_R = 4.3
POST_L = 8.4
POST_CUP_RIM = 4.15     # countersunk recess in the post end: radius at the rim
POST_CUP_R = 3.6        # radius of its flat floor
POST_CUP_D = 1.0        # depth
GUSSET_R = 8.5          # radial reach of gusset at the underside
GUSSET_H = 7.5          # height along post where gusset ends
GUSSET_T_IN = 2.2       # gusset thickness where it meets the post
GUSSET_T_OUT = 0.6      # gusset thickness at its outer edge
GUSSET_ANGLES = (180.0, 60.0, -60.0)

# large circular recess in the underside
REC_Y = 23.0
REC_R = 23.6
REC_D = 4.0
HUB_R = 4.25            # central boss left standing in the recess

# three arc slots in the recess floor, each with a pin
SLOT_R_IN = 10.0
SLOT_R_OUT = 17.7
SLOT_HALF_IN = 41.0     # half angle of the slot at the inner radius (deg)
SLOT_FLARE = 14.0       # end walls flare outward from radial by this (deg)
SLOT_CORNER_R = 3.0     # rounding of the outer slot corners
SLOT_D = 4.0            # depth below the recess floor
SLOT_ANGLES = (180.0, 60.0, -60.0)
PIN_RAD_POS = 10.9
PIN_R = 1.15

# two round blind pockets
POCKET_X = 19.5
POCKET_Y = -1.7
POCKET_R = 4.55
POCKET_D = 5.0

# ---------------- block ----------------
block = cq.Workplane("XY").box(BLOCK_X, BLOCK_Y, BLOCK_H, centered=(True, True, False))

# ---------------- recess + hub ----------------
recess = (cq.Workplane("XY").center(0, REC_Y).circle(REC_R).extrude(REC_D))
hub = (cq.Workplane("XY").center(0, REC_Y).circle(HUB_R).extrude(REC_D))
block = block.cut(recess).union(hub)

# ---------------- arc slots ----------------
def arc_slot(theta_c):
    """arc slot: inner arc between sharp corners at +-SLOT_HALF_IN, end walls
    flaring outward by SLOT_FLARE from radial, outer arc, rounded outer corners"""
    cx, cy = 0.0, REC_Y
    tc = math.radians(theta_c)

    def rot(pt):
        c, s_ = math.cos(tc), math.sin(tc)
        return (cx + pt[0] * c - pt[1] * s_, cy + pt[0] * s_ + pt[1] * c)

    def pol(r, a_deg):
        a = math.radians(a_deg)
        return (r * math.cos(a), r * math.sin(a))

    # corner points in the slot's local frame (slot centred on +x axis)
    pts = {}
    for sgn in (1, -1):
        a_in = sgn * SLOT_HALF_IN
        p0 = pol(SLOT_R_IN, a_in)
        d = pol(1.0, a_in + sgn * SLOT_FLARE)
        pd = p0[0] * d[0] + p0[1] * d[1]
        t = -pd + math.sqrt(pd * pd - (SLOT_R_IN ** 2 - SLOT_R_OUT ** 2))
        p1 = (p0[0] + t * d[0], p0[1] + t * d[1])
        pts[sgn] = (p0, p1)
    (i_p, o_p), (i_m, o_m) = pts[1], pts[-1]
    wp = (cq.Workplane("XY").workplane(offset=REC_D)
          .moveTo(*rot(i_m))
          .lineTo(*rot(o_m))
          .threePointArc(rot((SLOT_R_OUT, 0.0)), rot(o_p))
          .lineTo(*rot(i_p))
          .threePointArc(rot((SLOT_R_IN, 0.0)), rot(i_m))
          .close()
          .extrude(SLOT_D))
    shp = wp.val()
    outer = []
    for e in shp.Edges():
        if e.geomType() != "LINE":
            continue
        a, b = e.startPoint(), e.endPoint()
        if abs(a.z - b.z) < 1e-6:
            continue
        if math.hypot(a.x - cx, a.y - cy) > 0.5 * (SLOT_R_IN + SLOT_R_OUT):
            outer.append(e)
    shp = shp.fillet(SLOT_CORNER_R, outer)
    return cq.Workplane("XY").add(shp)

for th in SLOT_ANGLES:
    block = block.cut(arc_slot(th))

# pins standing in the slots, ending flush with the underside
for th in SLOT_ANGLES:
    a = math.radians(th)
    px, py = PIN_RAD_POS * math.cos(a), REC_Y + PIN_RAD_POS * math.sin(a)
    pin = cq.Workplane("XY").center(px, py).circle(PIN_R).extrude(REC_D + SLOT_D)
    block = block.union(pin)

# ---------------- round pockets ----------------
pockets = (cq.Workplane("XY")
           .pushPoints([(POCKET_X, POCKET_Y), (-POCKET_X, POCKET_Y)])
           .circle(POCKET_R).extrude(POCKET_D))
block = block.cut(pockets)

# ---------------- post with gussets ----------------
post = (cq.Workplane("XY").circle(POST_R).extrude(-POST_L)
        .rotate((0, 0, 0), (0, 0, 1), 180.0)      # hide the cylinder seam under a gusset
        .translate((0, POST_Y, 0)))

# gusset: concave profile in the radial (r, z) plane; in plan view it is a
# wedge, thick where it meets the post and thin at its outer edge
def gusset(angle_deg):
    side = (cq.Workplane("XZ")
            .moveTo(POST_R - 0.5, 0.5)
            .lineTo(GUSSET_R, 0.5)
            .lineTo(GUSSET_R, 0.0)
            .threePointArc((POST_R + 1.35, -GUSSET_H * 0.52), (POST_R - 0.01, -GUSSET_H))
            .lineTo(POST_R - 0.5, -GUSSET_H)
            .close()
            .extrude(GUSSET_T_IN, both=True))
    r0, r1 = POST_R, GUSSET_R
    k = (GUSSET_T_OUT - GUSSET_T_IN) / (2.0 * (r1 - r0))      # half-thickness slope
    ra, rb = r0 - 1.0, r1 + 0.5
    ha, hb = GUSSET_T_IN / 2 + k * (ra - r0), GUSSET_T_IN / 2 + k * (rb - r0)
    wedge = (cq.Workplane("XY").workplane(offset=-GUSSET_H - 0.5)
             .polyline([(ra, -ha), (rb, -hb), (rb, hb), (ra, ha)])
             .close()
             .extrude(GUSSET_H + 1.0))
    g = side.intersect(wedge)
    return g.rotate((0, 0, 0), (0, 0, 1), angle_deg).translate((0, POST_Y, 0))

for ang in GUSSET_ANGLES:
    post = post.union(gusset(ang))

# shallow conical (countersunk) recess in the end of the post
ext = 0.2
slope = (POST_CUP_RIM - POST_CUP_R) / POST_CUP_D
cup = cq.Solid.makeCone(POST_CUP_RIM + ext * slope, POST_CUP_R, POST_CUP_D + ext,
                        cq.Vector(0, POST_Y, -POST_L - ext), cq.Vector(0, 0, 1))
post = post.cut(cq.Workplane("XY").add(cup))

result = block.union(post)

VIEW = {"azimuth": 45, "elevation": 26}
